import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
# Wall flange (disc) - lies in the XZ plane, front face at Y=0, back at +Y
DISC_D = 150.0
DISC_T = 5.8
DISC_EDGE_R = 1.5
BOLT_PCD_R = 62.0          # radius of the 4 small mounting holes
BOLT_D = 9.0
BOLT_CHAMFER = 0.4
BOSS_D = 13.0              # low pads around the mounting holes
BOSS_H = 0.65
CUT_R_IN = 37.7            # lightening cut-outs (4x on the diagonals)
CUT_R_OUT = 68.4
CUT_HALF_ANG = 30.5        # deg
CUT_FIL_IN = 13.9
CUT_FIL_OUT = 15.2
CUT_EDGE_R = 0.8

# Clevis bracket (extends toward -Y)
PLATE_T = 8.5
GAP = 17.5                 # clear gap between upper and lower plate
PLATE_LEN = 112.7          # from disc front face to plate front end
PLATE_EDGE_R = 1.6
PIN_Y = -73.0              # pin axis position
UP_W = 78.8                # upper plate wide part
NECK_W = 56.0              # upper plate neck width (= lower plate width)
UP_VTX_WIDE = -42.7        # S-curve polygon vertex on the wide edge (Y)
UP_VTX_NECK = -25.1        # S-curve polygon vertex on the neck edge (Y)
UP_S_R_WIDE = 11.0         # S-curve radius at the wide side
UP_S_R_NECK = 37.6         # S-curve radius at the neck side
UP_CORNER_R = 13.0
UP_HOLE_D = 8.0
UP_HOLE_CSK = 12.2
UP_HOLE_PITCH = 43.2
LOW_W = 56.0
LOW_HOLE_D = 6.0
LOW_HOLE_Y = -103.0

# web between the plates around the pin
WEB_X0 = -14.4
WEB_X1 = 19.7
WEB_HALF_LEN = 12.65       # half length at mid height
WEB_END_R = 9.2            # concave cylindrical end faces of the web
CROSS_HOLE_D = 10.0
CROSS_HOLE_CH = 1.2

GAP_FIL = 5.5              # rounded end of the slot between the plates at the disc
SLOT_WALL = 0.8
JUNCTION_R = 4.5           # fillet where the bracket meets the disc

# gussets
GUS_T = 6.2
UP_GUS_L = 6.0
UP_GUS_H = 27.7
LOW_GUS_L = 33.2
LOW_GUS_H = 28.1
GUS_R = 6.0

# pin
PIN_D = 11.5
PIN_HEAD_D = 20.0
PIN_HEAD_T = 5.8
PIN_TOP = 73.7
PIN_BOT = -38.6            # lower end of the pin
PIN_FLAT_TOP = -32.6       # flats on +/-X below this height
PIN_FLAT_W = 10.0          # across flats
PIN_GROOVE_W = 1.0
PIN_GROOVE_DEPTH = 0.8

VIEW = {"azimuth": 45, "elevation": 26}

# derived
ZU0 = GAP / 2.0               # underside of upper plate
ZU1 = GAP / 2.0 + PLATE_T     # top of upper plate
ZL0 = -GAP / 2.0              # top of lower plate
ZL1 = -GAP / 2.0 - PLATE_T    # bottom of lower plate
YF = -PLATE_LEN               # front end of plates


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def xcyl(r, x0, x1, y, z):
    """cylinder along X"""
    return (cq.Workplane("YZ", origin=(x0, 0, 0)).center(y, z)
            .circle(r).extrude(x1 - x0))


def zcyl(r, z0, z1, x, y):
    return cq.Workplane("XY", origin=(0, 0, z0)).center(x, y).circle(r).extrude(z1 - z0)


def box(x0, x1, y0, y1, z0, z1):
    x0, x1 = min(x0, x1), max(x0, x1)
    y0, y1 = min(y0, y1), max(y0, y1)
    z0, z1 = min(z0, z1), max(z0, z1)
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0).translate(
        ((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2))


def fillet_poly(wp, pts, radii):
    """Closed polygon on workplane wp with a tangent-arc fillet of radius
    radii[i] at vertex i (0 = sharp corner)."""
    n = len(pts)
    segs = []
    for i in range(n):
        p0 = pts[i - 1]
        p1 = pts[i]
        p2 = pts[(i + 1) % n]
        r = radii[i]
        if r <= 0:
            segs.append((p1, None, p1))
            continue
        d1 = (p1[0] - p0[0], p1[1] - p0[1])
        l1 = math.hypot(*d1)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (p2[0] - p1[0], p2[1] - p1[1])
        l2 = math.hypot(*d2)
        d2 = (d2[0] / l2, d2[1] / l2)
        cosang = -(d1[0] * d2[0] + d1[1] * d2[1])
        theta = math.acos(max(-1.0, min(1.0, cosang)))   # interior angle
        t = r / math.tan(theta / 2)
        a = (p1[0] - d1[0] * t, p1[1] - d1[1] * t)
        b = (p1[0] + d2[0] * t, p1[1] + d2[1] * t)
        bis = (-d1[0] + d2[0], -d1[1] + d2[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        dm = r / math.sin(theta / 2) - r
        m = (p1[0] + bis[0] * dm, p1[1] + bis[1] * dm)
        segs.append((a, m, b))
    w = wp.moveTo(*segs[0][2])
    for i in range(1, n + 1):
        a, m, b = segs[i % n]
        w = w.lineTo(*a)
        if m is not None:
            w = w.threePointArc(m, b)
    return w.close()


class EdgeFilter(cq.Selector):
    """select edges with a python predicate"""

    def __init__(self, pred):
        self.pred = pred

    def filter(self, objs):
        return [e for e in objs if self.pred(e)]


DEBUG = False


def try_fillet(wp, pred, r, tag=""):
    """fillet the selected edges; fall back to slightly smaller radii if the
    kernel refuses (deterministic)"""
    for k in (1.0, 0.93, 0.85, 0.7, 0.5):
        try:
            sel = wp.edges(EdgeFilter(pred))
            n = len(sel.vals())
            res = sel.fillet(r * k)
            if res.val().isValid():
                if DEBUG:
                    print("fillet ok", tag, n, r * k)
                return res
        except Exception:
            pass
    if DEBUG:
        print("fillet failed", tag)
    return wp


def _bb(e):
    return e.BoundingBox()


# ---------------------------------------------------------------------------
# Disc (wall flange)
# ---------------------------------------------------------------------------
disc = cq.Workplane("XZ").circle(DISC_D / 2).extrude(-DISC_T)   # Y 0..DISC_T
disc = disc.edges().fillet(DISC_EDGE_R)


def sector_cutter():
    """filleted annular sector prism along Y (centred on +X axis)"""
    a = math.radians(CUT_HALF_ANG)
    big = CUT_R_OUT * 1.6
    wedge = (cq.Workplane("XZ", origin=(0, 10, 0))
             .polyline([(0, 0), (big * math.cos(a), big * math.sin(a)),
                        (big * math.cos(a), -big * math.sin(a))]).close()
             .extrude(20 + DISC_T))
    ring = (cq.Workplane("XZ", origin=(0, 10, 0)).circle(CUT_R_OUT)
            .circle(CUT_R_IN).extrude(20 + DISC_T))
    s = ring.intersect(wedge)
    rmid = (CUT_R_IN + CUT_R_OUT) / 2

    def along_y(e, inner):
        c = e.Center()
        d = e.endPoint() - e.startPoint()
        return (abs(d.x) < 1e-6 and abs(d.z) < 1e-6
                and (math.hypot(c.x, c.z) < rmid) == inner)

    s = s.edges(EdgeFilter(lambda e: along_y(e, True))).fillet(CUT_FIL_IN)
    s = s.edges(EdgeFilter(lambda e: along_y(e, False))).fillet(CUT_FIL_OUT)
    return s


sc = sector_cutter()
for k in range(4):
    disc = disc.cut(sc.rotate((0, 0, 0), (0, 1, 0), 45 + 90 * k))

# soften the cut-out edges
disc = try_fillet(
    disc,
    lambda e: (CUT_R_IN - 1 < math.hypot(e.Center().x, e.Center().z) < CUT_R_OUT + 1
               and e.geomType() != "LINE" or
               (e.geomType() == "LINE" and abs((e.endPoint() - e.startPoint()).y) < 1e-6
                and CUT_R_IN - 1 < math.hypot(e.Center().x, e.Center().z) < CUT_R_OUT + 1)),
    CUT_EDGE_R, "cut")

# small mounting holes on the spokes (0, 90, 180, 270 deg), each with a low
# raised pad on both faces of the disc
for k in range(4):
    ang = math.radians(90 * k)
    x = BOLT_PCD_R * math.cos(ang)
    z = BOLT_PCD_R * math.sin(ang)
    pad = (cq.Workplane("XZ", origin=(0, DISC_T + BOSS_H, 0)).center(x, z)
           .circle(BOSS_D / 2).extrude(DISC_T + 2 * BOSS_H))
    disc = disc.union(pad)
disc = try_fillet(
    disc,
    lambda e: (e.geomType() == "CIRCLE" and abs(e.radius() - BOSS_D / 2) < 0.01
               and (abs(e.Center().y + BOSS_H) < 0.01
                    or abs(e.Center().y - DISC_T - BOSS_H) < 0.01)),
    BOSS_H * 0.5, "pad")
for k in range(4):
    ang = math.radians(90 * k)
    x = BOLT_PCD_R * math.cos(ang)
    z = BOLT_PCD_R * math.sin(ang)
    hole = (cq.Workplane("XZ", origin=(0, DISC_T + 5, 0)).center(x, z)
            .circle(BOLT_D / 2).extrude(DISC_T + 10))
    disc = disc.cut(hole)
disc = try_fillet(
    disc,
    lambda e: (e.geomType() == "CIRCLE" and abs(e.radius() - BOLT_D / 2) < 0.01
               and abs(math.hypot(e.Center().x, e.Center().z) - BOLT_PCD_R) < 1.0),
    BOLT_CHAMFER, "bolt")

# ---------------------------------------------------------------------------
# Upper plate: wide mounting part, S-curve, neck into the disc
# ---------------------------------------------------------------------------
up_pts = [(UP_W / 2, YF), (UP_W / 2, UP_VTX_WIDE), (NECK_W / 2, UP_VTX_NECK),
          (NECK_W / 2, 1.0), (-NECK_W / 2, 1.0), (-NECK_W / 2, UP_VTX_NECK),
          (-UP_W / 2, UP_VTX_WIDE), (-UP_W / 2, YF)]
up_rad = [UP_CORNER_R, UP_S_R_WIDE, UP_S_R_NECK, 0, 0, UP_S_R_NECK, UP_S_R_WIDE,
          UP_CORNER_R]
upper = fillet_poly(cq.Workplane("XY", origin=(0, 0, ZU0)), up_pts, up_rad).extrude(PLATE_T)
upper = try_fillet(upper, lambda e: _bb(e).ymin < -3 and
                   abs((e.endPoint() - e.startPoint()).z) < 1e-6 and
                   _bb(e).zlen < 1e-6, PLATE_EDGE_R, "upper")

# ---------------------------------------------------------------------------
# Lower plate: round-ended tongue
# ---------------------------------------------------------------------------
lr = LOW_W / 2
lower = (cq.Workplane("XY", origin=(0, 0, ZL1))
         .moveTo(lr, 1.0).lineTo(lr, YF + lr)
         .threePointArc((0, YF), (-lr, YF + lr))
         .lineTo(-lr, 1.0).close().extrude(PLATE_T))
lower = try_fillet(lower, lambda e: _bb(e).ymin < -3 and _bb(e).zlen < 1e-6,
                   PLATE_EDGE_R, "lower")

# ---------------------------------------------------------------------------
# Web between the plates around the pin (concave front/back faces)
# ---------------------------------------------------------------------------
yf = PIN_Y - WEB_HALF_LEN
yb = PIN_Y + WEB_HALF_LEN
h = GAP / 2
_wext = math.sqrt(WEB_END_R ** 2 - h ** 2)     # arc meets the plates at an angle
web = box(WEB_X0, WEB_X1, yf - (WEB_END_R - _wext) - 0.5, yb + (WEB_END_R - _wext) + 0.5,
          -h - 0.2, h + 0.2)
web = web.cut(xcyl(WEB_END_R, WEB_X0 - 1, WEB_X1 + 1, yf - WEB_END_R, 0))
web = web.cut(xcyl(WEB_END_R, WEB_X0 - 1, WEB_X1 + 1, yb + WEB_END_R, 0))

# closed end of the slot between the plates at the disc (rounded slot end,
# leaving a thin wall SLOT_WALL in front of the disc face)
_ge = GAP_FIL + SLOT_WALL
_gz = h + PLATE_EDGE_R + 0.3
gf = box(-NECK_W / 2, NECK_W / 2, -_ge, 0.5, -_gz, _gz)
gf = gf.cut(box(-NECK_W / 2 - 1, NECK_W / 2 + 1, -_ge - 1, -SLOT_WALL,
                -(h - GAP_FIL), h - GAP_FIL))
for zz in (h - GAP_FIL, -(h - GAP_FIL)):
    gf = gf.cut(xcyl(GAP_FIL, -NECK_W / 2 - 1, NECK_W / 2 + 1, -_ge, zz))

# ---------------------------------------------------------------------------
# Gussets (triangular ribs above and below)
# ---------------------------------------------------------------------------
up_gus = (cq.Workplane("YZ", origin=(-GUS_T / 2, 0, 0))
          .polyline([(0.5, ZU1 - 1.0), (-UP_GUS_L, ZU1 - 1.0), (-UP_GUS_L, ZU1),
                     (0.5, ZU1 + UP_GUS_H)]).close().extrude(GUS_T))
low_gus = (cq.Workplane("YZ", origin=(-GUS_T / 2, 0, 0))
           .polyline([(0.5, ZL1 + 1.0), (-LOW_GUS_L, ZL1 + 1.0), (-LOW_GUS_L, ZL1),
                      (0.5, ZL1 - LOW_GUS_H)]).close().extrude(GUS_T))

# concave blends where the sides of the neck meet the disc (full height)
_jz0 = ZL1 + 0.5 * PLATE_EDGE_R
_jz1 = ZU1 - 0.5 * PLATE_EDGE_R
jstrips = None
for sx in (-1, 1):
    xs = sx * NECK_W / 2
    st = box(xs, xs + sx * JUNCTION_R, -JUNCTION_R, 0.5, _jz0, _jz1)
    st = st.cut(zcyl(JUNCTION_R, _jz0 - 1, _jz1 + 1, xs + sx * JUNCTION_R, -JUNCTION_R))
    jstrips = st if jstrips is None else jstrips.union(st)

body = (disc.union(upper).union(lower).union(gf).union(jstrips)
        .union(up_gus).union(low_gus)).clean()


def gusset_edge(e):
    """concave edges where the gussets sit on the plates (not on the disc)"""
    bb = _bb(e)
    if bb.ymin > -0.05:                  # edges lying in the disc face
        return False
    if bb.ymax > 0.05:
        return False
    on_plate = (abs(bb.zmin - ZU1) < 0.05 and abs(bb.zmax - ZU1) < 0.05) or \
               (abs(bb.zmin - ZL1) < 0.05 and abs(bb.zmax - ZL1) < 0.05)
    return on_plate and bb.xmin > -GUS_T / 2 - 0.05 and bb.xmax < GUS_T / 2 + 0.05


body = try_fillet(body, gusset_edge, GUS_R, "gusset")

body = body.union(web)

# ---------------------------------------------------------------------------
# Holes in the plates
# ---------------------------------------------------------------------------
for sx in (-1, 1):
    for sy in (-1, 1):
        x = sx * UP_HOLE_PITCH / 2
        y = PIN_Y + sy * UP_HOLE_PITCH / 2
        body = body.cut(zcyl(UP_HOLE_D / 2, ZU0 - 1, ZU1 + 1, x, y))
        cs_h = (UP_HOLE_CSK - UP_HOLE_D) / 2
        cs = (cq.Workplane("XY", origin=(x, y, ZU1 - cs_h))
              .circle(UP_HOLE_D / 2).workplane(offset=cs_h + 0.5)
              .circle(UP_HOLE_CSK / 2 + 0.5).loft())
        body = body.cut(cs)

# pin hole through both plates and the web (slightly larger than the pin)
body = body.cut(zcyl(PIN_D / 2 + 0.3, ZL1 - 1, ZU1 + 1, 0, PIN_Y))
cs = (cq.Workplane("XY", origin=(0, PIN_Y, ZU1 - 1.5)).circle(PIN_D / 2 + 0.3)
      .workplane(offset=2.0).circle(PIN_D / 2 + 2.3).loft())
body = body.cut(cs)
# small hole in the lower plate tongue
body = body.cut(zcyl(LOW_HOLE_D / 2, ZL1 - 1, ZL0 + 1, 0, LOW_HOLE_Y))
# cross hole through the web along X, chamfered both ends
body = body.cut(xcyl(CROSS_HOLE_D / 2, WEB_X0 - 1, WEB_X1 + 1, PIN_Y, 0))
for xe, sgn in ((WEB_X0, 1), (WEB_X1, -1)):
    cone = (cq.Workplane("YZ", origin=(xe - sgn * 0.5, 0, 0)).center(PIN_Y, 0)
            .circle(CROSS_HOLE_D / 2 + CROSS_HOLE_CH + 0.5)
            .workplane(offset=sgn * (CROSS_HOLE_CH + 0.5)).circle(CROSS_HOLE_D / 2).loft())
    body = body.cut(cone)

# ---------------------------------------------------------------------------
# Pin with head and nut
# ---------------------------------------------------------------------------
pin = zcyl(PIN_D / 2, PIN_BOT, PIN_TOP - PIN_HEAD_T + 0.01, 0, PIN_Y)
pin = pin.faces("<Z").edges().chamfer(0.8)
head = (zcyl(PIN_HEAD_D / 2, PIN_TOP - PIN_HEAD_T, PIN_TOP, 0, PIN_Y)
        .edges().chamfer(1.0))
pin = pin.union(head)
# retaining groove and spanner flats at the lower end
_gz0 = PIN_FLAT_TOP
pin = pin.cut(zcyl(PIN_D / 2 + 1, _gz0, _gz0 + PIN_GROOVE_W, 0, PIN_Y)
              .cut(zcyl(PIN_D / 2 - PIN_GROOVE_DEPTH, _gz0 - 1, _gz0 + PIN_GROOVE_W + 1, 0, PIN_Y)))
for sx in (-1, 1):
    pin = pin.cut(box(sx * PIN_FLAT_W / 2, sx * (PIN_D / 2 + 2), PIN_Y - PIN_D, PIN_Y + PIN_D,
                      PIN_BOT - 1, _gz0))

result = body.union(pin)
